"""Fluted control knob: 24 rounded flutes, a large rounded top edge over which the flutes run out,
flat top, flat bottom with a blind D-shaft bore."""
import math
import cadquery as cq
from OCP.BRep import BRep_Tool
from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeFace, BRepBuilderAPI_Sewing
from OCP.Geom import Geom_BSplineSurface, Geom_TrimmedCurve
from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
from OCP.ShapeFix import ShapeFix_Solid
from OCP.TColgp import TColgp_Array2OfPnt
from OCP.TColStd import TColStd_Array1OfInteger, TColStd_Array1OfReal, TColStd_Array2OfReal
from OCP.gp import gp_Pnt

# ---------------- driving dimensions (mm) ----------------
N_FLUTES = 24          # number of flutes (lobes) around the knob
R_OUT = 13.0           # radius at the lobe crests
R_IN = 12.43           # radius at the valley bottoms (valleys on the X and Y axes)
HEIGHT = 20.0          # overall height
TOP_ROUND = 4.2        # radius of the rounded top edge, followed by the crests
HOLE_D = 6.0           # D-shaft bore diameter
HOLE_FLAT = 1.5        # distance from the bore axis to the flat (flat toward +Y)
HOLE_DEPTH = 12.0      # blind bore depth from the bottom face
SEAM_ANGLE = 90.0      # valley where the closed side surface starts / ends (deg)

# ---------------- fluted outline: convex lobe arcs and concave valley arcs, tangent ----------------
# Lobe arc (radius r, centre at R_OUT - r) and valley arc (radius r, centre at R_IN + r, half a pitch
# away) must touch: |c_lobe - c_valley| = 2 r, a quadratic in r.
th = math.pi / N_FLUTES                     # half pitch
cth = math.cos(th)
_a = 2.0 * (cth - 1.0)
_b = -2.0 * (R_OUT - R_IN) * (1.0 + cth)
_c = R_OUT ** 2 + R_IN ** 2 - 2.0 * cth * R_OUT * R_IN
R_ARC = (-_b - math.sqrt(_b * _b - 4.0 * _a * _c)) / (2.0 * _a)   # lobe radius = valley radius
C_LOBE = R_OUT - R_ARC                      # pitch radius of the lobe-arc centres
C_VAL = R_IN + R_ARC                        # pitch radius of the valley-arc centres
A0 = math.radians(SEAM_ANGLE)


def pol(r, ang):
    return cq.Vector(r * math.cos(ang), r * math.sin(ang), 0.0)


def touch(c_lobe, c_val):
    """Tangency point of a lobe arc and a valley arc."""
    d = c_val - c_lobe
    return c_lobe + d * (R_ARC / d.Length)


def valley_mid(c_val, p, q):
    """Point on the valley arc (centre c_val) halfway between p and q."""
    return c_val - (c_val - (p + q) * 0.5).normalized() * R_ARC


def outline_edges():
    """Closed outline beginning and ending at the bottom of the valley at SEAM_ANGLE."""
    edges = []
    for k in range(N_FLUTES):
        gv = A0 + 2 * th * k               # this valley
        gl = gv + th                       # lobe
        gn = gv + 2 * th                   # next valley
        cl = pol(C_LOBE, gl)
        t0 = touch(cl, pol(C_VAL, gv))
        t1 = touch(cl, pol(C_VAL, gn))
        if k == 0:                         # rising half of the seam valley
            vb = pol(R_IN, gv)
            edges.append(cq.Edge.makeThreePointArc(vb, valley_mid(pol(C_VAL, gv), vb, t0), t0))
        edges.append(cq.Edge.makeThreePointArc(t0, pol(R_OUT, gl), t1))
        vb = pol(R_IN, gn)
        if k < N_FLUTES - 1:
            t2 = touch(pol(C_LOBE, gn + th), pol(C_VAL, gn))
            edges.append(cq.Edge.makeThreePointArc(t1, vb, t2))
        else:                              # falling half of the seam valley
            edges.append(cq.Edge.makeThreePointArc(t1, valley_mid(pol(C_VAL, gn), t1, vb), vb))
    return edges


def join_to_nurbs(edges):
    """The tangent arc chain as one exact (rational) B-spline curve."""
    comp = None
    for e in edges:
        f, l = BRep_Tool.Range_s(e.wrapped)
        tc = Geom_TrimmedCurve(BRep_Tool.Curve_s(e.wrapped, 0.0, 0.0), f, l)
        if comp is None:
            comp = GeomConvert_CompCurveToBSplineCurve(tc)
        else:
            comp.Add(tc, 1e-7)
    return comp.BSplineCurve()


outline = join_to_nurbs(outline_edges())

# ---------------- side + rounded crown: the outline swept up a straight wall and over a quarter round ----------
# Sweep law in (scale, z): straight wall to z0, then a quarter round of radius TOP_ROUND followed by the crests;
# the whole outline is scaled about the axis, so the flutes run out over the round onto the flat top.
z0 = HEIGHT - TOP_ROUND
s_top = (R_OUT - TOP_ROUND) / R_OUT
LAW_POLES = [(1.0, 0.0), (1.0, 0.5 * z0), (1.0, z0), (1.0, HEIGHT), (s_top, HEIGHT)]
LAW_WEIGHTS = [1.0, 1.0, 1.0, math.sqrt(0.5), 1.0]
LAW_KNOTS, LAW_MULTS = [0.0, 1.0, 2.0], [3, 2, 3]


def arr1(vals, cls):
    a = cls(1, len(vals))
    for i, v in enumerate(vals, start=1):
        a.SetValue(i, v)
    return a


nu, nv = outline.NbPoles(), len(LAW_POLES)
poles = TColgp_Array2OfPnt(1, nu, 1, nv)
weights = TColStd_Array2OfReal(1, nu, 1, nv)
for i in range(1, nu + 1):
    p, w = outline.Pole(i), outline.Weight(i)
    for j, ((s, z), wv) in enumerate(zip(LAW_POLES, LAW_WEIGHTS), start=1):
        poles.SetValue(i, j, gp_Pnt(p.X() * s, p.Y() * s, z))
        weights.SetValue(i, j, w * wv)
side_srf = Geom_BSplineSurface(
    poles, weights,
    arr1([outline.Knot(i) for i in range(1, outline.NbKnots() + 1)], TColStd_Array1OfReal),
    arr1(LAW_KNOTS, TColStd_Array1OfReal),
    arr1([outline.Multiplicity(i) for i in range(1, outline.NbKnots() + 1)], TColStd_Array1OfInteger),
    arr1(LAW_MULTS, TColStd_Array1OfInteger),
    outline.Degree(), 2, False, False)
# extra knots along the height (shape unchanged) give the mesher an even grid over wall and crown
for k in range(1, 8):
    side_srf.InsertVKnot(k / 8.0, 1, 1e-9)
for k in range(1, 16):
    side_srf.InsertVKnot(1.0 + k / 16.0, 1, 1e-9)
side = cq.Face(BRepBuilderAPI_MakeFace(side_srf, 1e-7).Face())


def rim(face, z):
    return cq.Wire.assembleEdges([cq.Edge(e.wrapped) for e in face.Edges()
                                  if abs(e.Center().z - z) < 1e-6 and e.Length() > 1.0])


bottom = cq.Face.makeFromWires(rim(side, 0.0))
top = cq.Face.makeFromWires(rim(side, HEIGHT))

sew = BRepBuilderAPI_Sewing(1e-5)
for f in (side, bottom, top):
    sew.Add(f.wrapped)
sew.Perform()
fix = ShapeFix_Solid(cq.Solid.makeSolid(cq.Shell(sew.SewedShape())).wrapped)
fix.Perform()
knob = cq.Workplane("XY").add(cq.Solid(fix.Solid()))

# ---------------- blind D-shaft bore from the bottom ----------------
keep = HOLE_FLAT + HOLE_D / 2.0 + 1.0      # strip keeping the round part of the D
bore = (cq.Workplane("XY")
        .circle(HOLE_D / 2.0).extrude(HOLE_DEPTH)
        .intersect(cq.Workplane("XY")
                   .center(0, HOLE_FLAT - keep / 2.0)
                   .rect(HOLE_D * 1.2, keep)
                   .extrude(HOLE_DEPTH)))
knob = knob.cut(bore)

result = knob
